import cadquery as cq
import math

# =====================================================================
#  Curved arm with a cup at one end and a low chamfered disk at the
#  other (e.g. a mixer / tap lever arm).  X = long axis, Z = up.
# =====================================================================

# ---------------- cup end (-X) ----------------
RING_R = 25.0          # outer radius of the cup
BORE_R = 22.8          # cup bore radius (thin wall)
CUP_FLOOR = 4.0        # cup floor height
CUP_FLOOR_R = 3.0      # fillet between bore wall and floor
FOOT_Z = 5.6           # the foot band of the cup is stepped in slightly
FOOT_R = 24.5
RING_FOOT_CH = 0.6     # chamfer at the foot of the cup

# lobe: flat-floored tongue shaped recess running from the cup into the arm
LOBE_C = (27.5, 5.5)   # centre of the rounded end of the lobe
LOBE_R = 12.0
LOBE_FLOOR = 27.5      # floor height at the pad
LOBE_RAMP = 20.0       # floor rises toward +X (deg)

# ---------------- disk end (+X) ----------------
DISK_X = 189.0
DISK_Y = 1.0
DISK_R = 22.5
DISK_Z0 = 2.7          # disk bottom
DISK_Z1 = 14.7         # disk top (flat)
DISK_TOP_R = 16.5      # radius of the flat top (cone chamfer outside)
DISK_CH_Z = 8.1        # height where the cone chamfer meets the cylinder

# ---------------- arm ----------------
TOP_FILLET_NEG = 8.0  # large round on the -Y (front) top edge of the arm
TOP_FILLET_POS = 6.0   # tighter round on the +Y (back) top edge
BOT_FILLET = 4.0
KINK_X = 151.5         # arm top turns down toward the disk here
X_END = 187.0          # arm body runs into the disk up to here
HOOD_END_R = 7.0       # rounding of the sloped hood at the disk end

# side profile (XZ) of the upper surface of the arm / cup rim
TOP_PTS = [(-32.0, 22.5), (-25.0, 25.8), (-10.0, 31.5), (10.0, 36.0), (31.0, 39.0),
           (55.0, 40.0), (80.0, 40.2), (105.0, 39.5), (127.0, 38.1), (KINK_X, 34.5)]
SLOPE_END = (X_END, DISK_Z1)
# lower surface of the arm (dips below the disk bottom at the end, trimmed later)
BOT_PTS = [(-5.0, 6.5), (17.0, 8.1), (49.6, 11.1), (85.0, 12.3), (118.9, 11.5),
           (142.0, 9.7), (160.6, 5.7), (174.5, 3.2), (X_END, 1.0)]
BOT_TAN = [(-1, 0.18), (-1, -0.07)]
BOT_TRIM_X = 140.0

# plan outline (XY) of the arm: +Y edge and -Y edge
POS_EDGE = [(-5.0, 24.2), (24.0, 26.1), (74.0, 28.3), (124.0, 27.0), (151.0, 24.8),
            (172.0, 23.8), (X_END, 23.4)]
NEG_EDGE = [(-5.0, -23.5), (14.6, -21.3), (35.0, -16.1), (55.7, -12.0), (74.0, -9.0),
            (99.0, -7.2), (124.0, -7.5), (140.0, -8.3), (151.0, -9.6), (X_END, -21.4)]
NEG_KINK = 8           # index of the crease where the hood flank starts

# U-shaped scoop in the sloped end over the disk
SCOOP_C = (165.5, 6.2)   # centre of the rounded back of the scoop
SCOOP_R = 9.5
SCOOP_TOP_SLOPE = -0.11  # the +Y side of the scoop closes in slightly toward the disk
SCOOP_SPLAY = 0.48       # the -Y side of the scoop opens toward the disk
SCOOP_TAPER = 3.0        # draft of the scoop walls (deg)
SCOOP_FLOOR = DISK_Z1

# oblong bosses on top of the arm: (x, y, top z)
BOSS_L, BOSS_W = 13.0, 9.2
BOSSES = [(69.3, 9.6, 41.3), (126.4, 9.5, 41.5)]
PIN_D = 1.2
PIN_SPACING = 5.5

# raised arrow / size marking between lobe and first boss
MARK_X, MARK_Y, MARK_TOP = 51.0, 8.2, 40.9

# flat pad in the scoop: (x, y, z, length, width)
SCOOP_PAD = (162.2, 4.6, SCOOP_FLOOR, 14.0, 8.7)
LOBE_PAD = (26.6, 5.4, 12.0, 15.5, 9.2)   # x, y, angle, length, width
PAD_H = 1.2

# locating tabs under the arm: (x0, x1, y0, y1, z_bottom)
TAB_RING = (24.6, 34.5, -3.7, 5.3, -1.9)
TAB_DISK = (162.5, 173.4, 10.4, 19.4, -5.1)


# ---------------------------------------------------------------------
def top_region(wp, close_low=-20.0, x_end=230.0):
    """XZ region below the upper surface line (used to trim the cup rim)."""
    return (wp.moveTo(TOP_PTS[0][0], close_low)
            .lineTo(*TOP_PTS[0])
            .spline(TOP_PTS[1:], includeCurrent=True)
            .lineTo(*SLOPE_END)
            .lineTo(x_end, SLOPE_END[1])
            .lineTo(x_end, close_low)
            .close())


def side_profile_solid(width=120.0):
    """Closed XZ outline of the arm (top + bottom), extruded along Y."""
    wp = cq.Workplane("XZ", origin=(0, width / 2.0, 0))
    s = (wp.moveTo(*BOT_PTS[0])
         .lineTo(TOP_PTS[0][0], BOT_PTS[0][1])
         .lineTo(*TOP_PTS[0])
         .spline(TOP_PTS[1:], includeCurrent=True)
         .lineTo(*SLOPE_END)
         .lineTo(*BOT_PTS[-1])
         .spline(list(reversed(BOT_PTS[:-1])), tangents=BOT_TAN, includeCurrent=True)
         .close())
    return s.extrude(width)


def plan_band_solid(h=80.0):
    wp = cq.Workplane("XY").workplane(offset=-10)
    s = (wp.moveTo(*POS_EDGE[0])
         .spline(POS_EDGE[1:], includeCurrent=True)
         .lineTo(*NEG_EDGE[-1])
         .lineTo(*NEG_EDGE[NEG_KINK])      # straight, flared flank of the hood
         .spline(list(reversed(NEG_EDGE[:NEG_KINK])), includeCurrent=True)
         .close())
    return s.extrude(h)


def fillet_edges(wpobj, radius, pred):
    sh = wpobj.val()
    edges = [e for e in sh.Edges() if pred(e.BoundingBox())]
    return cq.Workplane("XY").newObject([sh.fillet(radius, edges)])


def arch_wire(x, y0, y1, ztop, zbot, r0, r1):
    """Cross-section (YZ plane at x) with rounded upper corners r0 (-Y), r1 (+Y)."""
    c = math.cos(math.radians(45))
    return (cq.Workplane("YZ", origin=(x, 0, 0))
            .moveTo(y0, zbot).lineTo(y1, zbot).lineTo(y1, ztop - r1)
            .threePointArc((y1 - r1 + r1 * c, ztop - r1 + r1 * c), (y1 - r1, ztop))
            .lineTo(y0 + r0, ztop)
            .threePointArc((y0 + r0 - r0 * c, ztop - r0 + r0 * c), (y0, ztop - r0))
            .close()).val()


def stadium(x, y, ang, z0, length, width, h):
    """Obround pad, long axis along Y rotated by ang (deg) about Z."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y)
            .transformed(rotate=(0, 0, ang))
            .slot2D(length, width, 90)
            .extrude(h))


def pin_pts(x, y, ang):
    a = math.radians(ang)
    return [(x - math.sin(a) * s * PIN_SPACING / 2.0, y + math.cos(a) * s * PIN_SPACING / 2.0)
            for s in (-1, 1)]


def pin_holes(x, y, ang, z_top, depth):
    return (cq.Workplane("XY").workplane(offset=z_top - depth)
            .pushPoints(pin_pts(x, y, ang)).circle(PIN_D / 2.0).extrude(depth + 1))


def disk_revolve(r_bot, z0, z_ch, r_top, z1):
    return (cq.Workplane("XZ", origin=(DISK_X, DISK_Y, 0))
            .moveTo(0, z0)
            .lineTo(r_bot, z0)
            .lineTo(r_bot, z_ch)
            .lineTo(r_top, z1)
            .lineTo(0, z1)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- arm ----------------
arm = plan_band_solid().intersect(side_profile_solid())
arm = fillet_edges(arm, BOT_FILLET,
                   lambda b: b.zmax < 14 and (b.xmax - b.xmin > 100 or
                                              (b.xmin > KINK_X - 2 and b.xmax > X_END - 1
                                               and b.ymax < -5 and b.zmax < 10)))
arm = fillet_edges(arm, TOP_FILLET_NEG,
                   lambda b: (b.xmin < 0 and b.xmax > 140 and b.zmax > 38 and b.ymin < -5))
arm = fillet_edges(arm, TOP_FILLET_POS,
                   lambda b: (b.xmin < 0 and b.xmax > 140 and b.zmax > 38 and b.ymin > 20))

# rounded top edges of the sloped hood: intersect with a ruled loft whose
# section goes from the arm section at the kink to a low arch at the disk
kink_y1 = POS_EDGE[4][1]
kink_y0 = NEG_EDGE[NEG_KINK][1]
end_x = DISK_X
end_top = TOP_PTS[-1][1] + (end_x - KINK_X) * (SLOPE_END[1] - TOP_PTS[-1][1]) / (SLOPE_END[0] - KINK_X)
w_kink = arch_wire(KINK_X, kink_y0 - 0.2, kink_y1 + 0.2, TOP_PTS[-1][1] + 0.2, -10,
                   TOP_FILLET_NEG, TOP_FILLET_POS)
w_end = arch_wire(end_x, -22.6, 23.7, end_top + 0.2, -10, HOOD_END_R + 2.0, HOOD_END_R - 2.0)
hood_env = cq.Workplane("XY").newObject([cq.Solid.makeLoft([w_kink, w_end], True)])
hood_keep = hood_env.union(box(KINK_X - 250, KINK_X, -60, 60, -40, 80))
arm = arm.intersect(hood_keep)

# ---------------- cup end ----------------
top_trim = top_region(cq.Workplane("XZ", origin=(0, 60, 0))).extrude(120)
ring = (cq.Workplane("XY").circle(FOOT_R).extrude(FOOT_Z + 1.0)
        .faces("<Z").edges().chamfer(RING_FOOT_CH)
        .union(cq.Workplane("XY").workplane(offset=FOOT_Z).circle(RING_R).extrude(60))
        .intersect(top_trim))

# ---------------- disk end ----------------
disk = disk_revolve(DISK_R, DISK_Z0, DISK_CH_Z, DISK_TOP_R, DISK_Z1)

body = arm.union(ring).union(disk)
# flat underside of the disk end
body = body.cut(box(BOT_TRIM_X, BOT_TRIM_X + 120, -60, 60, DISK_Z0 - 30, DISK_Z0))

# ---------------- bosses and marking on top ----------------
for (bx, by, btop) in BOSSES:
    body = body.union(stadium(bx, by, 0.0, 25.0, BOSS_L, BOSS_W, btop - 25.0))

mark = (cq.Workplane("XY").workplane(offset=30.0)
        .polyline([(MARK_X - 2.6, MARK_Y + 3.6), (MARK_X + 2.6, MARK_Y + 3.6),
                   (MARK_X, MARK_Y + 8.2)]).close()
        .polyline([(MARK_X - 2.6, MARK_Y - 3.6), (MARK_X + 2.6, MARK_Y - 3.6),
                   (MARK_X, MARK_Y - 8.2)]).close()
        .extrude(MARK_TOP - 30.0))
mark = mark.union(box(MARK_X - 1.6, MARK_X + 1.6, MARK_Y - 2.8, MARK_Y + 2.8, 30.0, MARK_TOP - 0.2))
body = body.union(mark)

# ---------------- cup bore ----------------
bore = (cq.Workplane("XZ", origin=(0, 0, 0))
        .moveTo(0, CUP_FLOOR)
        .lineTo(BORE_R - CUP_FLOOR_R, CUP_FLOOR)
        .radiusArc((BORE_R, CUP_FLOOR + CUP_FLOOR_R), -CUP_FLOOR_R)
        .lineTo(BORE_R, 70)
        .lineTo(0, 70)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
body = body.cut(bore)

# ---------------- lobe ----------------
dx, dy = LOBE_C
d = math.hypot(dx, dy)
ux, uy = dx / d, dy / d
ca = (BORE_R - LOBE_R) / d
sa = math.sqrt(1 - ca * ca)
hull_pts = []
for sgn in (1, -1):
    tx = ux * ca - sgn * uy * sa
    ty = uy * ca + sgn * ux * sa
    hull_pts.append(((BORE_R * tx, BORE_R * ty), (dx + LOBE_R * tx, dy + LOBE_R * ty)))
lobe = (cq.Workplane("XY").workplane(offset=0.0)
        .moveTo(*hull_pts[1][0])
        .lineTo(*hull_pts[1][1])
        .threePointArc((dx + LOBE_R * ux, dy + LOBE_R * uy), hull_pts[0][1])
        .lineTo(*hull_pts[0][0])
        .threePointArc((-BORE_R * ux, -BORE_R * uy), hull_pts[1][0])
        .close()
        .extrude(70))
lx, ly, la, ll, lw = LOBE_PAD
above_ramp = (cq.Workplane("XY").box(300, 300, 100, centered=(True, True, False))
              .rotate((0, 0, 0), (0, 1, 0), -LOBE_RAMP)
              .translate((lx, ly, LOBE_FLOOR)))
body = body.cut(lobe.intersect(above_ramp))

# pad with two pins on the ramp floor
ramp_plane = cq.Plane(origin=(lx, ly, LOBE_FLOOR),
                      xDir=(math.cos(math.radians(LOBE_RAMP)), 0, math.sin(math.radians(LOBE_RAMP))),
                      normal=(-math.sin(math.radians(LOBE_RAMP)), 0, math.cos(math.radians(LOBE_RAMP))))
lobe_pad = (cq.Workplane(ramp_plane).workplane(offset=-1.0)
            .transformed(rotate=(0, 0, la))
            .slot2D(ll, lw, 90).extrude(PAD_H + 1.0))
body = body.union(lobe_pad)
lobe_pins = (cq.Workplane(ramp_plane).workplane(offset=PAD_H - 2.0)
             .transformed(rotate=(0, 0, la))
             .pushPoints([(0, -PIN_SPACING / 2.0), (0, PIN_SPACING / 2.0)])
             .circle(PIN_D / 2.0).extrude(3.0))
body = body.cut(lobe_pins)

# ---------------- scoop over the disk ----------------
scx, scy = SCOOP_C
a_end = math.radians(255.0)
p_end = (scx + SCOOP_R * math.cos(a_end), scy + SCOOP_R * math.sin(a_end))
x_far = DISK_X + 30
scoop = (cq.Workplane("XY").workplane(offset=SCOOP_FLOOR)
         .moveTo(x_far, scy + SCOOP_R + (x_far - scx) * SCOOP_TOP_SLOPE)
         .lineTo(scx, scy + SCOOP_R)
         .threePointArc((scx - SCOOP_R, scy), p_end)
         .lineTo(x_far, p_end[1] - (x_far - p_end[0]) * SCOOP_SPLAY)
         .close()
         .extrude(30, taper=-SCOOP_TAPER))
body = body.cut(scoop)

px, py, pz, pl, pw = SCOOP_PAD
body = body.union(stadium(px, py, 0.0, pz - 0.5, pl, pw, PAD_H + 0.5))
body = body.cut(pin_holes(px, py, 0.0, pz + PAD_H, 2.0))

for (bx, by, btop) in BOSSES:
    body = body.cut(pin_holes(bx, by, 0.0, btop, 3.0))

# ---------------- tabs under the arm ----------------
x0, x1, y0, y1, zb = TAB_RING
tab = box(x0, x1, y0, y1, zb, 11.0)
tab = tab.cut(box(x0 - 1, x1 + 1, (y0 + y1) / 2 - 0.9, (y0 + y1) / 2 + 0.9, zb - 1, zb + 1.8))
tab = tab.cut(box(x0 - 1, x0 + 1.8, y0 - 1, y1 + 1, zb - 1, zb + 1.5))
body = body.union(tab)

x0, x1, y0, y1, zb = TAB_DISK
tab = box(x0, x1, y0, y1, zb, 11.0)
tab = tab.cut(cq.Workplane("XY").workplane(offset=zb - 1)
              .center((x0 + x1) / 2 + 1.5, (y0 + y1) / 2).circle(1.6).extrude(4.0))
body = body.union(tab)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
